import math
import cadquery as cq
from cadquery import Vector as V
from OCP.Geom import Geom_BSplineSurface
from OCP.TColgp import TColgp_Array2OfPnt
from OCP.TColStd import (TColStd_Array2OfReal, TColStd_Array1OfReal,
                         TColStd_Array1OfInteger)
from OCP.gp import gp_Pnt
from OCP.BRepBuilderAPI import (BRepBuilderAPI_MakeFace, BRepBuilderAPI_Sewing,
                                BRepBuilderAPI_MakeEdge, BRepBuilderAPI_MakeWire,
                                BRepBuilderAPI_MakeSolid)
from OCP.TopoDS import TopoDS
from OCP.TopAbs import TopAbs_SHELL
from OCP.TopExp import TopExp_Explorer

# ---------------- driving dimensions (mm) ----------------
L = 124.0          # overall length of the obround socket
R_E = 29.3         # radius of the two rounded ends of the socket body
S_F = 2.05         # outward bow of the front face (flush with the spigot)
H = 121.0          # overall height
D = 62.7           # outside diameter of the round spigot
DB = 54.0          # bore of the round spigot
E = 0.0            # spigot axis offset towards the back (+Y)
Z_P1 = 65.0        # outer transition profile (at the ends): upper corner
Z_P2 = 34.4        # outer transition profile (at the ends): lower corner
R_P1 = 15.6        # convex blend radius at the upper corner
R_P2 = 17.7        # concave blend radius at the lower corner
T_SOCK = 7.2       # wall thickness of the obround socket
S_FI = 1.3         # bow of the socket front wall
SOCK_DEPTH = 53.0  # depth of the straight socket below the top face
FLOOR_DROP = 11.2  # drop of the sloped socket floor (about 22 deg)
ENTRY_DROP = 6.0   # extra drop of the rounded entry into the bore
ENTRY_R = 3.5      # entry round at the top inside edge
GROOVE_TOP = 8.6   # depth of the internal groove below the top face
GROOVE_H = 3.3     # height of the groove (vertical back wall)
GROOVE_D = 1.2     # depth of the groove (radial), bottom is a 45 deg chamfer
BORE_CH = 0.6      # chamfer at the bottom inside edge of the spigot
TXT = "SUBEA RC1"
TXT_SIZE = 9.0
TXT_DEPTH = 0.4
TXT_Z = H - 20.5   # height of the text centre line

R0 = R_E                     # end radius of the obround
A_T = L / 2.0 - R0           # half distance between the end-arc centres
RT = D / 2.0                 # spigot radius
RS = R0 - T_SOCK             # inner end radius of the socket
RB = DB / 2.0                # bore radius
Z_F = H - SOCK_DEPTH         # bottom of the straight socket

C45 = math.cos(math.radians(45.0))


# ---------------- helpers: obround -> circle transition surfaces ----------
def front_arc(a, r, s):
    """Circle through (-a, -r), (0, -r - s), (a, -r): radius and centre y."""
    rf = (a * a + s * s) / (2.0 * s)
    return rf, -r - s + rf


def obround_poles(a, r, s=0.0, seam_back=True):
    """Rational quadratic control polygon of the socket section (8 spans,
    CCW, starting at the front centre): bowed front, round ends, flat back."""
    if s > 1e-9:
        rf, yc = front_arc(a, r, s)
        th = math.asin(a / rf)
        x1 = rf * math.tan(th / 2.0)
        front = [((0, -r - s), 1.0), ((x1, -r - s), math.cos(th / 2.0))]
    else:
        front = [((0, -r), 1.0), ((a / 2, -r), 1.0)]
    h = front + [((a, -r), 1.0),
                 ((a + r, -r), C45), ((a + r, 0), 1.0), ((a + r, r), C45),
                 ((a, r), 1.0), ((a / 2, r), 1.0), ((0, r), 1.0)]
    full = h + [((-p[0], p[1]), w) for (p, w) in reversed(h[:-1])]
    # the surface seam goes where it is least seen: outside at the back
    # centre, inside at the front centre
    return full[8:] + full[1:9] if seam_back else full


def circle_poles(r, cy, alpha, seam_back=True):
    """Circle split into 8 rational spans that correspond to the obround
    spans (alpha = angle matched to the half straight side)."""
    angs = [-90, -90 + alpha, 0, 90 - alpha, 90, 90 + alpha, 180,
            270 - alpha, 270]
    out = []
    for i in range(8):
        t0, t1 = math.radians(angs[i]), math.radians(angs[i + 1])
        tm, dl = (t0 + t1) / 2, (t1 - t0)
        if i == 0:
            out.append(((r * math.cos(t0), cy + r * math.sin(t0)), 1.0))
        rm = r / math.cos(dl / 2)
        out.append(((rm * math.cos(tm), cy + rm * math.sin(tm)),
                    math.cos(dl / 2)))
        out.append(((r * math.cos(t1), cy + r * math.sin(t1)), 1.0))
    return out[8:] + out[1:9] if seam_back else out


def blend_rows(p, q, t):
    return [(((1 - t) * a[0][0] + t * b[0][0], (1 - t) * a[0][1] + t * b[0][1]),
             (1 - t) * a[1] + t * b[1]) for a, b in zip(p, q)]


def nurbs_face(rows, zs, nref):
    """Face of a NURBS surface: rational quadratic around (u, 8 spans),
    cubic along the height with Bezier segments (4 rows, sharing ends)."""
    nu, nv = len(rows[0]), len(rows)
    nseg = (nv - 1) // 3
    poles = TColgp_Array2OfPnt(1, nu, 1, nv)
    wts = TColStd_Array2OfReal(1, nu, 1, nv)
    for j in range(nv):
        for i, ((x, y), w) in enumerate(rows[j]):
            poles.SetValue(i + 1, j + 1, gp_Pnt(x, y, zs[j]))
            wts.SetValue(i + 1, j + 1, w)
    uk = TColStd_Array1OfReal(1, 9)
    um = TColStd_Array1OfInteger(1, 9)
    for i in range(9):
        uk.SetValue(i + 1, float(i))
        um.SetValue(i + 1, 3 if i in (0, 8) else 2)
    vk = TColStd_Array1OfReal(1, nseg + 1)
    vm = TColStd_Array1OfInteger(1, nseg + 1)
    for k in range(nseg + 1):
        vk.SetValue(k + 1, float(k))
        vm.SetValue(k + 1, 4 if k in (0, nseg) else 3)
    surf = Geom_BSplineSurface(poles, wts, uk, vk, um, vm, 2, 3, False, False)
    # extra knots only refine the parametrisation (finer, cleaner meshing)
    for seg in range(nseg):
        n = nref[seg]
        for k in range(1, n):
            surf.InsertVKnot(seg + k / float(n), 1, 1e-9, True)
    for k in range(8):
        for q in range(1, 5):
            surf.InsertUKnot(k + q / 5.0, 1, 1e-9, True)
    return surf, BRepBuilderAPI_MakeFace(surf, 1e-7).Face()


def transition_solid(rows, zs, breaks=()):
    """Closed solid bounded by NURBS side faces that are cubic in height
    (consecutive groups of four control rows, sharing their end rows, form
    Bezier segments; a new face starts at every segment index in `breaks`,
    i.e. at sharp creases) and flat caps at the top and bottom."""
    nseg = (len(rows) - 1) // 3
    cuts = [0] + sorted(breaks) + [nseg]
    sew = BRepBuilderAPI_Sewing(1e-5)
    surfs = []
    for a, b in zip(cuts[:-1], cuts[1:]):
        r, z = rows[3 * a:3 * b + 1], zs[3 * a:3 * b + 1]
        nref = [max(2, min(8, int(abs(z[3 * k] - z[3 * k + 3]) / 1.5) + 2))
                for k in range(b - a)]
        sf, fc = nurbs_face(r, z, nref)
        surfs.append(sf)
        sew.Add(fc)
    for sf, v in ((surfs[0], 0.0), (surfs[-1], None)):
        if v is None:
            v = sf.VKnot(sf.NbVKnots())
        edge = BRepBuilderAPI_MakeEdge(sf.VIso(v)).Edge()
        wire = BRepBuilderAPI_MakeWire(edge).Wire()
        sew.Add(BRepBuilderAPI_MakeFace(wire, True).Face())
    sew.Perform()
    exp = TopExp_Explorer(sew.SewedShape(), TopAbs_SHELL)
    solid = BRepBuilderAPI_MakeSolid(TopoDS.Shell_s(exp.Current())).Solid()
    s = cq.Solid(solid).fix()
    if s.Volume() < 0:
        s = cq.Solid(solid.Reversed())
    return s


def s_profile(x1, x2, z1, z2, r1, r2):
    """Cubic Bezier control points (blend factor f, height z) of the
    transition seen at the ends: vertical, convex round r1 at corner
    (x1, z1), straight slope, concave round r2 at corner (x2, z2),
    vertical.  f = 0 is the obround, f = 1 the circle."""
    ux, uz = x2 - x1, z2 - z1
    ln = math.hypot(ux, uz)
    ux, uz = ux / ln, uz / ln
    ang = math.acos(-uz)                      # bend angle at each corner
    t1, t2 = r1 * math.tan(ang / 2), r2 * math.tan(ang / 2)
    k1 = 4.0 / 3.0 * math.tan(ang / 4) * r1
    k2 = 4.0 / 3.0 * math.tan(ang / 4) * r2
    a0 = (x1, z1 + t1)
    a1 = (x1 + ux * t1, z1 + uz * t1)
    b0 = (x2 - ux * t2, z2 - uz * t2)
    b1 = (x2, z2 - t2)
    pts = [a0, (a0[0], a0[1] - k1), (a1[0] - ux * k1, a1[1] - uz * k1), a1,
           (a1[0] + (b0[0] - a1[0]) / 3, a1[1] + (b0[1] - a1[1]) / 3),
           (a1[0] + 2 * (b0[0] - a1[0]) / 3, a1[1] + 2 * (b0[1] - a1[1]) / 3),
           b0, (b0[0] + ux * k2, b0[1] + uz * k2), (b1[0], b1[1] + k2), b1]
    return [((x1 - x) / (x1 - x2), z) for (x, z) in pts]


def match_angle(a, r):
    """Circle angle matched to the half straight side (arc length ratio)."""
    return 180.0 * a / (2.0 * (a + math.pi * r / 2.0))


# ---------------- outer body ----------------
# One smooth side wall, bottom to top: straight obround body with a bowed
# front, an S shaped blend (vertical tangents at both ends) into the round
# spigot, then the straight spigot.
ob_o = obround_poles(A_T, R0, S_F)
ci_o = circle_poles(RT, E, match_angle(A_T, R0))
prof = s_profile(L / 2.0, RT, Z_P1, Z_P2, R_P1, R_P2)
Z_T, Z_B = prof[0][1], prof[-1][1]
hs, hp = (H - Z_T) / 3.0, Z_B / 3.0
outer = transition_solid(
    [ob_o, ob_o, ob_o] + [blend_rows(ob_o, ci_o, f) for f, z in prof]
    + [ci_o, ci_o, ci_o],
    [H, H - hs, H - 2 * hs] + [z for f, z in prof]
    + [Z_B - hp, Z_B - 2 * hp, 0.0])

# ---------------- cavity ----------------
# One smooth inside wall, top to bottom: rounded entry, straight socket,
# sloped floor rounding into the bore, straight bore, bottom chamfer.
ci_i = circle_poles(RB, E, match_angle(A_T, RS), False)


def sock(d):
    """Socket section pushed outwards by d."""
    return obround_poles(A_T, RS + d, S_FI, False)


def bore_sec(d):
    """Bore section pushed outwards by d."""
    return circle_poles(RB + d, E, match_angle(A_T, RS), False)


# entry round: arc of radius ENTRY_R tangent to the socket wall, crossing
# the top face at a steep angle (85 deg of arc, the top face cuts it at 80)
phi = math.radians(85.0)
k_r = 4.0 / 3.0 * math.tan(phi / 4.0) * ENTRY_R
z0 = H - ENTRY_R * math.sin(math.radians(80.0))
d3 = ENTRY_R * (1.0 - math.cos(phi))
z3 = z0 + ENTRY_R * math.sin(phi)
d2 = d3 - k_r * math.sin(phi)
z2 = z3 - k_r * math.cos(phi)
z_fl = Z_F - FLOOR_DROP
z_bt = z_fl - ENTRY_DROP
z_gt = H - GROOVE_TOP                  # groove: square top
z_gm = z_gt - GROOVE_H                 # groove: bottom of the back wall
z_gb = z_gm - GROOVE_D                 # groove: end of the 45 deg chamfer


def seg_line(p, q):
    """Interior Bezier rows of a straight segment between (d, z) points."""
    return [(p[0] + (q[0] - p[0]) * t, p[1] + (q[1] - p[1]) * t)
            for t in (1 / 3.0, 2 / 3.0)]


# (offset d, height z) control points of the socket part, top to bottom
sk = [(d3, H + 1.0)] + seg_line((d3, H + 1.0), (d3, z3)) + [(d3, z3)]
sk += [(d2, z2), (0.0, z0 + k_r), (0.0, z0)]                 # entry round
sk += seg_line((0.0, z0), (0.0, z_gt)) + [(0.0, z_gt)]       # wall
sk += seg_line((0.0, z_gt), (GROOVE_D, z_gt)) + [(GROOVE_D, z_gt)]  # groove
sk += seg_line((GROOVE_D, z_gt), (GROOVE_D, z_gm)) + [(GROOVE_D, z_gm)]
sk += seg_line((GROOVE_D, z_gm), (0.0, z_gb)) + [(0.0, z_gb)]
sk += seg_line((0.0, z_gb), (0.0, Z_F)) + [(0.0, Z_F)]       # wall
hb = (z_bt - BORE_CH) / 3.0
hc = (BORE_CH + 1.0) / 3.0
cavity = transition_solid(
    [sock(d) for d, z in sk]
    + [blend_rows(sock(0.0), ci_i, 0.5), ci_i,                # sloped floor
       ci_i, ci_i, ci_i,                                       # bore
       ci_i, bore_sec(hc), bore_sec(2 * hc), bore_sec(3 * hc)],  # chamfer
    [z for d, z in sk]
    + [Z_F - FLOOR_DROP / 2, z_fl,
       z_bt, z_bt - hb, z_bt - 2 * hb,
       BORE_CH, BORE_CH - hc, BORE_CH - 2 * hc, -1.0],
    # separate faces at the sharp creases: groove corners, floor edge, chamfer
    breaks=(3, 4, 5, 6, 7, 9))

body = cq.Workplane("XY").add(outer.cut(cavity))

# mirrored engraving on the (slightly bowed) front face: the letters are cut
# to a constant depth below the face
txt_plane = cq.Plane(origin=(0, 0, TXT_Z), xDir=(-1, 0, 0), normal=(0, 1, 0))
txt = (cq.Workplane(txt_plane)
       .text(TXT, TXT_SIZE, -(R0 + S_F + 5.0), font="DejaVu Sans",
             kind="bold", combine=False)).val()
skin = outer.translate(V(0, -2.0, 0)).cut(outer.translate(V(0, TXT_DEPTH, 0)))
body = body.cut(txt.intersect(skin))

result = body
